import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Jumbo-roll dispenser back shell (open toward -Y, back face at +Y)
# X = width, Z = height, Y = depth.  Main circle centre at X=0, Z=0.
# ---------------------------------------------------------------------------

# overall outline
R = 143.0            # outer radius of the round upper body
XN = 83.0            # half width of the neck at its narrowest point
ZN = -176.0          # height of the narrowest point of the neck
ZB = -212.5          # bottom corners of the neck
ZM = -187.5          # top of the concave bottom edge (middle)
D = 70.5             # total depth (front rim to back face)
T = 11.25            # side wall thickness
TF = 11.25           # floor (back plate) thickness
RF = 9.5             # fillet on the back outer edge
RS_IN = 165.0        # radius of the inner step arc (seen from the front)
RS_OUT = 167.0       # radius of the outer step arc (seen from the back)
S = 10.5             # the lower band is set forward by this amount

# central hub (raised frustum on the floor)
HUB_RB = 40.6        # base radius
HUB_RT = 26.9        # top radius
HUB_H = 12.0         # height above floor
HUB_HOLE = 22.5      # central through hole
HEX_X = 24.0         # hex nut pockets offset
HEX_D = 14.4         # across corners
HEX_DEPTH = 6.0
HEX_HOLE = 5.0

# ribs / bars
BAR_W = 73.5
BAR_H = 12.6
BAR_P = 11.0         # protrusion from floor
BAR_LIP = 3.0        # front lip thickness
BAR_GD = 3.0         # groove depth behind the lip
BAR_END = 6.0        # solid end blocks
BAR1_Z = -88.8
BAR2_Z = -177.0

# snap catches on the inner side walls of the neck
WB_Z = -177.0
WB_H = 12.0
WB_W = 17.5          # protrusion from the wall
WB_Y = 10.0          # front face of the catch (from the front rim plane)

# band holes
BH_X = 63.0
BH_Z1 = -162.5
BH_Z2 = -191.5
BH_D = 6.0

# top bracket
TB1_W = 22.5
TB1_ZB = 109.6
TB1_P = 43.5
TB2_W = 40.5
TB2_ZB = 96.0
TB2_P = 23.5
TB1_HZ = 121.0       # hole in the narrow block
TB1_HD = 8.5
TB2_HX = 11.2        # holes in the wide block
TB2_HZ = 103.0
TB2_HD = 6.5

YF = D - TF            # floor front surface (main area)
YFB = D - S - TF       # floor front surface (lower band)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0)
            .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)))


def ycyl(x, z, r, y0, y1):
    return cq.Workplane("XY").add(
        cq.Solid.makeCylinder(r, y1 - y0, cq.Vector(x, y0, z), cq.Vector(0, 1, 0)))


# --- derived outline geometry ------------------------------------------------
RC = (XN ** 2 + ZN ** 2 - R ** 2) / (2 * (R - XN))   # concave neck radius
CX = XN + RC                                           # neck arc centre (right)
CZ = ZN
dist = math.hypot(CX, CZ)
TX, TZ = R * CX / dist, R * CZ / dist                 # tangent point (right)
BX = CX - math.sqrt(RC ** 2 - (ZB - CZ) ** 2)          # bottom corner (right)


def outer_profile():
    return (cq.Workplane("XZ")
            .moveTo(TX, TZ)
            .threePointArc((0, R), (-TX, TZ))
            .threePointArc((-XN, ZN), (-BX, ZB))
            .threePointArc((0, ZM), (BX, ZB))
            .threePointArc((XN, ZN), (TX, TZ))
            .close())


def inner_profile():
    ri = R - T
    rci = RC + T
    tix, tiz = ri * CX / dist, ri * CZ / dist
    zlow = ZB - 25.0
    xlow = CX - math.sqrt(rci ** 2 - (zlow - CZ) ** 2)
    return (cq.Workplane("XZ")
            .moveTo(tix, tiz)
            .threePointArc((0, ri), (-tix, tiz))
            .threePointArc((-(XN - T), ZN), (-xlow, zlow))
            .lineTo(xlow, zlow)
            .threePointArc((XN - T, ZN), (tix, tiz))
            .close())


# --- main shell --------------------------------------------------------------
body = outer_profile().extrude(-D)          # Y from 0 to D
body = body.faces(">Y").edges().fillet(RF)

# step: the lower band is set forward by S
step_cut = box(-300, 300, D - S, D + 5, -400, 0).cut(ycyl(0, 0, RS_OUT, D - S - 1, D + 10))
body = body.cut(step_cut)

# cavity
cav = inner_profile().extrude(-YF)
band_fill = box(-300, 300, YFB, YF, -400, 0).cut(ycyl(0, 0, RS_IN, YFB - 1, YF + 1))
cav = cav.cut(band_fill)
body = body.cut(cav)

# --- central hub --------------------------------------------------------------
hub = cq.Workplane("XY").add(
    cq.Solid.makeCone(HUB_RB, HUB_RT, HUB_H + 1.0,
                      cq.Vector(0, YF + 1.0, 0), cq.Vector(0, -1, 0)))
body = body.union(hub)
ytop = YF - HUB_H
for sx in (-1, 1):
    hexp = (cq.Workplane("XZ", origin=(0, ytop, 0))
            .center(sx * HEX_X, 0).polygon(6, HEX_D).extrude(-HEX_DEPTH))
    body = body.cut(hexp)
    body = body.cut(ycyl(sx * HEX_X, 0, HEX_HOLE / 2, ytop - 1, D + 5))
body = body.cut(ycyl(0, 0, HUB_HOLE / 2, -5, D + 10))

# --- bars on the floor (front lip with a groove behind it, solid ends) -------
for zc, yf in ((BAR1_Z, YF), (BAR2_Z, YFB)):
    bar = box(-BAR_W / 2, BAR_W / 2, yf - BAR_P, yf + 0.5,
              zc - BAR_H / 2, zc + BAR_H / 2)
    for sz in (-1, 1):
        z_out = zc + sz * (BAR_H / 2 + 1.0)
        z_in = zc + sz * (BAR_H / 2 - BAR_GD)
        groove = box(-BAR_W / 2 + BAR_END, BAR_W / 2 - BAR_END,
                     yf - BAR_P + BAR_LIP, yf + 0.1, min(z_in, z_out), max(z_in, z_out))
        bar = bar.cut(groove)
    body = body.union(bar)

# --- snap catches (wedges) on the inner side walls of the neck -------------
for sx in (-1, 1):
    xw = XN - T + 4.0          # a little inside the wall material
    wedge = (cq.Workplane("XY", origin=(0, 0, WB_Z - WB_H / 2))
             .polyline([(xw, WB_Y), (xw - 4.0 - WB_W, WB_Y), (xw, WB_Y + WB_W + 4.0)])
             .close().extrude(WB_H))
    if sx < 0:
        wedge = wedge.mirror("YZ")
    body = body.union(wedge)

# band holes
for sx in (-1, 1):
    for zz in (BH_Z1, BH_Z2):
        body = body.cut(ycyl(sx * BH_X, zz, BH_D / 2, YFB - 5, D + 5))

# --- top bracket --------------------------------------------------------------
ztop_in = R - T
b1 = box(-TB1_W / 2, TB1_W / 2, YF - TB1_P, YF + 0.5, TB1_ZB, ztop_in + 3)
b2 = box(-TB2_W / 2, TB2_W / 2, YF - TB2_P, YF + 0.5, TB2_ZB, TB1_ZB)
body = body.union(b1).union(b2)
# holes in the front faces
body = body.cut(ycyl(0, TB1_HZ, TB1_HD / 2, YF - TB1_P - 1, YF - TB1_P + 14))
for sx in (-1, 1):
    body = body.cut(ycyl(sx * TB2_HX, TB2_HZ, TB2_HD / 2, YF - TB2_P - 1, YF - 1.0))
# nut slots in the bottom faces
body = body.cut(box(-5, 5, YF - TB1_P + 6, YF - TB1_P + 10, TB1_ZB - 1, TB1_ZB + 6))
for sx in (-1, 1):
    body = body.cut(box(sx * TB2_HX - 4, sx * TB2_HX + 4, YF - TB2_P + 6, YF - TB2_P + 10,
                        TB2_ZB - 1, TB2_ZB + 6))

# --- back bow-tie recess around the hub ---------------------------------------
BT_D = 36.0          # round part of the recess
BT_DEPTH_R = 10.0    # depth of the round part
BT_L = 68.0          # overall length of the wings
BT_W = 16.0          # height of the wings
BT_DEPTH = 4.0       # depth of the wings
bt = (cq.Workplane("XZ", origin=(0, D + 1.0, 0)).circle(BT_D / 2).extrude(BT_DEPTH_R + 1.0)
      .union(box(-BT_L / 2, BT_L / 2, D - BT_DEPTH, D + 1.0, -BT_W / 2, BT_W / 2)))
body = body.cut(bt)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
